import math
import cadquery as cq

# Trailer-hitch ball mount: a tapered shank carrying a hitch ball at the -X end,
# lightened by an X-ribbed through pocket, ending (+X) in a receiver box that is
# notched into a clevis (top plate, bottom plate, -Y side wall, inner end wall)
# with a pin hole through the bottom plate.

# ---------------- driving dimensions (mm) ----------------
L = 244.1          # overall length of the mount body (X)
W = 100.0          # overall width (Y)
H = 54.6           # height of the receiver box end (Z)
H_TIP = 29.7       # height of the shank at the ball end (underside is tapered)
X_BOX = 169.9      # start of the constant-height box section

# clevis notch in the box end (open towards +X and +Y)
T_TOP = 8.8        # top plate thickness
T_BOT = 8.8        # bottom plate thickness
T_WALL = 8.8       # side wall thickness (-Y side)
T_END = 8.8        # inner end wall thickness (starts at X_BOX)
HOLE_D = 13.0      # pin hole through the bottom plate
HOLE_X = 213.6
HOLE_Y = 0.0

# lightening pocket with two diagonal (corner to corner) ribs
P_X0 = 52.0        # pocket start (X)
P_X1 = 161.2       # pocket end (X)
P_HALF_Y = 41.0    # pocket half width (Y)
RIB_W = 9.0        # rib width

# hitch ball on a cylindrical neck, with a flat on top
BALL_X = 24.85
BALL_R = 27.5
BALL_FLAT_R = 15.0                      # radius of the flat on top of the ball
NECK_R = 17.2
BALL_TOP = 60.0                         # flat top height above the body top face
BALL_CZ = BALL_TOP - math.sqrt(BALL_R ** 2 - BALL_FLAT_R ** 2)  # ball centre above top face
SEAM_ANGLE = 135.0                      # park the periodic-surface seams at the back

# ---------------- shank body: tapered section + box section ----------------
z_tip_bot = H - H_TIP
taper = (
    cq.Workplane("XZ")
    .polyline([(0, z_tip_bot), (X_BOX, 0), (X_BOX, H), (0, H)]).close()
    .extrude(W / 2.0, both=True)
)
box_end = (
    cq.Workplane("XY")
    .box(L - X_BOX, W, H, centered=False)
    .translate((X_BOX, -W / 2.0, 0))
)
body = taper.union(box_end, clean=False)

# ---------------- clevis notch in the box end ----------------
notch_len = L - (X_BOX + T_END)
notch_w = W - T_WALL
notch_h = H - T_TOP - T_BOT
notch = (
    cq.Workplane("XY")
    .box(notch_len + 1.0, notch_w + 1.0, notch_h, centered=False)
    .translate((X_BOX + T_END, -W / 2.0 + T_WALL, T_BOT))
)
body = body.cut(notch, clean=False)

# pin hole through the bottom plate
hole = (
    cq.Workplane("XY")
    .circle(HOLE_D / 2.0)
    .extrude(T_BOT + 2.0)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE - 180.0)
    .translate((HOLE_X, HOLE_Y, -1.0))
)
body = body.cut(hole, clean=False)

# ---------------- X-ribbed lightening pocket (through) ----------------
pcx = (P_X0 + P_X1) / 2.0
pa = (P_X1 - P_X0) / 2.0
pb = P_HALF_Y
theta = math.degrees(math.atan2(pb, pa))
diag = 2.0 * math.hypot(pa, pb)
pocket = (
    cq.Workplane("XY")
    .box(2 * pa, 2 * pb, H + 2.0)
    .translate((pcx, 0, H / 2.0))
)
for ang in (theta, -theta):
    rib = (
        cq.Workplane("XY")
        .box(diag * 1.2, RIB_W, H + 4.0)
        .rotate((0, 0, 0), (0, 0, 1), ang)
        .translate((pcx, 0, H / 2.0))
    )
    pocket = pocket.cut(rib)
body = body.cut(pocket, clean=False)

# ---------------- hitch ball ----------------
neck = (
    cq.Workplane("XY")
    .circle(NECK_R)
    .extrude(BALL_CZ + 1.0)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    .translate((BALL_X, 0, H - 1.0))
)
ball = (
    cq.Workplane("XY")
    .sphere(BALL_R)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    .translate((BALL_X, 0, H + BALL_CZ))
)
flat_cut = (
    cq.Workplane("XY")
    .box(4 * BALL_R, 4 * BALL_R, 2 * BALL_R)
    .translate((BALL_X, 0, H + BALL_TOP + BALL_R))
)
ball = ball.union(neck).cut(flat_cut)

result = body.union(ball, clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
